import math
import cadquery as cq

# =====================================================================
#  Flow-field plate: thin flange plate with a raised back block that
#  carries a shallow pocket with inclined channel recesses and raised
#  stadium-shaped islands, an outlet slot with a port hole, a port hole
#  in the top face of the block and a 14-hole bolt pattern through all.
#
#  Orientation: plate lies in the XZ plane, front face at Y = 0 facing
#  -Y, the block sits on the back (+Y) side.
# =====================================================================

# ---------------- flange plate ----------------
PLATE_W = 100.0      # X
PLATE_H = 133.3      # Z
PLATE_T = 0.7        # Y thickness
PLATE_R = 8.0        # corner radius (edges parallel to Y)

# ---------------- back block ----------------
BLOCK_INSET = 10.0   # inset of block from plate edge (all sides)
BLOCK_D = 8.3        # block depth (Y) behind the plate
BLOCK_R = 4.0        # block corner radius

# ---------------- bolt holes ----------------
HOLE_D = 4.5
HOLE_COLS_TB = [-29.5, -9.8, 9.8, 29.5]     # top and bottom rows
HOLE_COLS_SIDE = [-29.5, 29.5]
HOLE_PITCH_Z = 23.1                          # vertical pitch of the hole rows
HOLE_Z0 = 0.2                                # height of the middle row

# ---------------- pocket in back face ----------------
POCKET_W = 46.0
POCKET_H = 79.6
POCKET_DEPTH = 0.8
POCKET_R = 1.0
POCKET_CX = 0.3      # pocket centre X (slightly off the bolt-pattern centre)

# ---------------- inclined channel recesses ----------------
CH_X0, CH_X1 = -19.7, 21.1   # X range of the channels (vertical ends)
CH_H = 11.5          # vertical height of a channel
CH1_H = 12.3         # the top channel is a little taller
CH_DEPTH = 2.0       # depth below pocket floor
CH_R = 1.5           # corner radius
CH_CLIP = 1.0        # channels stay this far inside the pocket outline
CH_SLOPE = -0.205    # dZ/dX of channels (rise toward -X)
CH1_SLOPE = -0.12    # the top channel is less inclined
CH_ZC = [29.15, 14.4, -2.2, -19.05, -35.6]   # channel centre heights at X = 0

# ---------------- stadium islands / outlet slot ----------------
ST_W = 3.6           # stadium width
ST_SLOPE = -0.27     # dZ/dX of stadium axes
ST_X = (-13.0, 15.6) # end-centre X range of the long islands
ST1_X = (2.7, 15.6)  # short island in top channel (end-centre X range)
ST_ZC = [30.8, 14.36, -2.5, -19.3]   # island axis heights at X = 0
OUT_X = (-12.3, 2.8)  # outlet slot end-centre X range
OUT_ZC = -36.4       # outlet slot centre height at X = 0
OUT_W = 4.2          # outlet slot width
OUT_DEPTH = 1.0
ISLAND_H = 2.0       # island height above channel floor
OUT_HOLE_D = 1.6
OUT_HOLE_DEPTH = 4.0

# ---------------- port in the top face of the block ----------------
PORT_D = 4.5
PORT_DEPTH = 14.0

VIEW = {"azimuth": 45, "elevation": 26}

# =====================================================================
block_w = PLATE_W - 2 * BLOCK_INSET
block_h = PLATE_H - 2 * BLOCK_INSET
back_y = PLATE_T + BLOCK_D            # back face of the block
floor_y = back_y - POCKET_DEPTH       # pocket floor
ch_floor_y = floor_y - CH_DEPTH       # channel floor


def wp(y):
    """XZ workplane located at depth y (normal -Y; local x = X, local y = Z)."""
    return cq.Workplane("XZ", origin=(0, y, 0))


# --- flange plate (extrude toward +Y) ---
plate = (
    wp(0).rect(PLATE_W, PLATE_H).extrude(-PLATE_T)
    .edges("|Y").fillet(PLATE_R)
)

# --- back block ---
block = (
    wp(PLATE_T).rect(block_w, block_h).extrude(-BLOCK_D)
    .edges("|Y").fillet(BLOCK_R)
)
body = plate.union(block)

# --- pocket ---
pocket = (
    wp(back_y).center(POCKET_CX, 0).rect(POCKET_W, POCKET_H).extrude(POCKET_DEPTH)
    .edges("|Y").fillet(POCKET_R)
)
body = body.cut(pocket)

# pocket footprint used to clip the channels
pocket_clip = (
    wp(back_y).center(POCKET_CX, 0).rect(POCKET_W - 2 * CH_CLIP, POCKET_H - 2 * CH_CLIP)
    .extrude(POCKET_DEPTH + CH_DEPTH + 1)
)


def channel(zc, slope, h):
    x0, x1 = CH_X0, CH_X1
    pts = [
        (x0, zc + slope * x0 - h / 2),
        (x1, zc + slope * x1 - h / 2),
        (x1, zc + slope * x1 + h / 2),
        (x0, zc + slope * x0 + h / 2),
    ]
    s = wp(floor_y + 0.2).polyline(pts).close().extrude(CH_DEPTH + 0.2)
    s = s.edges("|Y").fillet(CH_R)
    return s.intersect(pocket_clip)


def stadium(y, xa, xb, zc, slope, w, depth):
    """stadium whose end-arc centres lie on z = zc + slope*x at x = xa, xb."""
    ang = math.degrees(math.atan(slope))
    length = abs(xb - xa) / math.cos(math.radians(ang))
    xm = 0.5 * (xa + xb)
    zm = zc + slope * xm
    return wp(y).center(xm, zm).slot2D(length + w, w, angle=ang).extrude(depth)


for i, zc in enumerate(CH_ZC):
    slope = CH1_SLOPE if i == 0 else CH_SLOPE
    h = CH1_H if i == 0 else CH_H
    body = body.cut(channel(zc, slope, h))

for i, zs in enumerate(ST_ZC):
    if i == 0:
        xa, xb = ST1_X
    else:
        xa, xb = ST_X
    # raised island standing on the channel floor
    island = stadium(ch_floor_y, xa, xb, zs, ST_SLOPE, ST_W, -ISLAND_H)
    body = body.union(island)

# --- outlet slot (in the bottom channel) with port hole at its +X end ---
body = body.cut(stadium(ch_floor_y + 0.01, OUT_X[0], OUT_X[1], OUT_ZC, ST_SLOPE, OUT_W, OUT_DEPTH))
hx = OUT_X[1]
hz = OUT_ZC + ST_SLOPE * hx
out_hole = (
    wp(ch_floor_y - OUT_DEPTH + 0.01).center(hx, hz).circle(OUT_HOLE_D / 2).extrude(OUT_HOLE_DEPTH)
)
body = body.cut(out_hole)

# --- bolt holes through plate and block ---
z_top = HOLE_Z0 + 2 * HOLE_PITCH_Z
z_bot = HOLE_Z0 - 2 * HOLE_PITCH_Z
pts = [(x, z_top) for x in HOLE_COLS_TB] + [(x, z_bot) for x in HOLE_COLS_TB]
pts += [(x, HOLE_Z0 + k * HOLE_PITCH_Z) for x in HOLE_COLS_SIDE for k in (-1, 0, 1)]
holes = (
    wp(-1.0).pushPoints(pts).circle(HOLE_D / 2).extrude(-(back_y + 2.0))
)
body = body.cut(holes)

# --- port in the top face of the block ---
top_z = block_h / 2
port = (
    cq.Workplane("XY", origin=(0, PLATE_T + BLOCK_D / 2, top_z + 1.0))
    .circle(PORT_D / 2)
    .extrude(-(PORT_DEPTH + 1.0))
)
body = body.cut(port)

result = body
